import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# origin = wheel / axle centre, X = forward (fork opening), Y = axle, Z = up
WHEEL_R = 62.5          # wheel outer radius
TREAD_W = 29.4          # tyre width
SHOULDER_R = 10.3       # tyre shoulder radius (section)
SHOULDER_CX = 50.2      # radius at which the tyre is widest
HUB_W = 14.5            # hub face half width
HUB_C = 19.0            # hub face corner radius position
HUB_EDGE_R = 2.5        # rounding of hub face edge
WALL_R = 25.0           # foot of hub wall
WEB_W = 9.0             # half width of recessed web
WEB_FILLET = 3.0
FLANK_FILLET = 3.0
HUB_WASHER_R = 16.0     # large washer on hub face
HUB_WASHER_T = 1.5

STEM_X = -26.5          # swivel (kingpin) axis offset behind the axle
STEM_D = 13.0
STEM_TOP = 137.8

DOME_R = 27.0
DOME_Z0 = 84.1
DOME_Z1 = 99.6
RING_R = 28.7
RING_Z0 = 81.9
BAND_R = 27.6

FORK_TOP = 77.5         # top surface of fork top plate
SHROUD_R = 29.8         # rear wrap-around radius of fork
LEG_W = 26.0            # outer half spacing of fork legs
SHEET_T = 2.5           # fork sheet thickness
FORK_FRONT = 13.5       # front edge of legs (x)
LEG_END_R = 13.5        # rounded leg end radius around axle
REAR_CUT_Z = 69.2       # height of rear diagonal cut at the back of the wrap
BEND_R = 3.0            # outer bend radius between top plate and side walls
PLAN_BLEND_R = 10.0     # plan-view blend radius between legs and rear wrap

HOLE_D = 3.9            # small holes near top of legs
HOLE_X = 5.2
HOLE_Z = 67.5

NUT_AF = 13.6           # axle nut across flats
NUT_T = 5.5
WASHER_D = 18.0
AXLE_D = 8.0


# ---------------- wheel ----------------
def _find_verts(face, pts, tol=0.05):
    out = []
    for v in face.Vertices():
        p = v.Center()
        for (x, y) in pts:
            if abs(p.x - x) < tol and abs(p.y - y) < tol:
                out.append(v)
                break
    return out


def make_wheel():
    """revolved wheel section (x = radius, y = axial): hub boss, recessed web,
    tyre with shoulder radius and crown radius, filleted corners"""
    V = cq.Vector
    sh_c = (SHOULDER_CX, TREAD_W / 2 - SHOULDER_R)  # shoulder arc centre
    # crown radius chosen so the crown arc is tangent to both shoulder arcs
    A = WHEEL_R - SHOULDER_CX
    crown_r = (A * A + sh_c[1] ** 2 - SHOULDER_R ** 2) / (2.0 * (A - SHOULDER_R))
    crown_c = WHEEL_R - crown_r
    rj = sh_c[0] - math.sqrt(SHOULDER_R ** 2 - (WEB_W - sh_c[1]) ** 2)
    d = math.hypot(sh_c[0] - crown_c, sh_c[1])
    tpx = crown_c + crown_r * (sh_c[0] - crown_c) / d
    tpy = crown_r * sh_c[1] / d
    top = sh_c[1] + SHOULDER_R

    def P(x, y):
        return V(x, y, 0)

    E = [
        cq.Edge.makeLine(P(0, -HUB_W), P(HUB_C, -HUB_W)),
        cq.Edge.makeLine(P(HUB_C, -HUB_W), P(WALL_R, -WEB_W)),
        cq.Edge.makeLine(P(WALL_R, -WEB_W), P(rj, -WEB_W)),
        cq.Edge.makeThreePointArc(P(rj, -WEB_W), P(sh_c[0], -top), P(tpx, -tpy)),
        cq.Edge.makeThreePointArc(P(tpx, -tpy), P(WHEEL_R, 0), P(tpx, tpy)),
        cq.Edge.makeThreePointArc(P(tpx, tpy), P(sh_c[0], top), P(rj, WEB_W)),
        cq.Edge.makeLine(P(rj, WEB_W), P(WALL_R, WEB_W)),
        cq.Edge.makeLine(P(WALL_R, WEB_W), P(HUB_C, HUB_W)),
        cq.Edge.makeLine(P(HUB_C, HUB_W), P(0, HUB_W)),
        cq.Edge.makeLine(P(0, HUB_W), P(0, -HUB_W)),
    ]
    f = cq.Face.makeFromWires(cq.Wire.assembleEdges(E))
    f = f.fillet2D(HUB_EDGE_R, _find_verts(f, [(HUB_C, HUB_W), (HUB_C, -HUB_W)]))
    f = f.fillet2D(WEB_FILLET, _find_verts(f, [(WALL_R, WEB_W), (WALL_R, -WEB_W)]))
    f = f.fillet2D(FLANK_FILLET, _find_verts(f, [(rj, WEB_W), (rj, -WEB_W)]))
    solid = cq.Solid.revolve(f, 360, V(0, 0, 0), V(0, 1, 0))
    w = cq.Workplane("XY").add(solid)
    # put the revolve seam up under the fork where it is hidden
    return w.rotate((0, 0, 0), (0, 1, 0), -110)


# ---------------- swivel head ----------------
def make_head():
    band = (cq.Workplane("XY").workplane(offset=FORK_TOP - 0.01)
            .circle(BAND_R).extrude(RING_Z0 - FORK_TOP + 0.01))
    ring = (cq.Workplane("XY").workplane(offset=RING_Z0)
            .circle(RING_R).extrude(DOME_Z0 - RING_Z0))
    # dome: single smooth spline profile revolved about the kingpin axis
    # measured silhouette of the cap: (radius, height above cap base)
    prof = [(DOME_R, 0.0), (DOME_R - 0.5, 4.3), (DOME_R - 1.8, 7.5),
            (DOME_R - 3.4, 10.6), (DOME_R - 6.0, 13.7), (DOME_R - 9.6, 15.2),
            (0.0, DOME_Z1 - DOME_Z0)]
    dpts = [cq.Vector(r, 0, DOME_Z0 + h) for (r, h) in prof]
    dspl = cq.Edge.makeSpline(dpts, tangents=[cq.Vector(0, 0, 1), cq.Vector(-1, 0, 0)],
                              scale=True)
    d1 = cq.Edge.makeLine(cq.Vector(0, 0, DOME_Z1), cq.Vector(0, 0, DOME_Z0))
    d2 = cq.Edge.makeLine(cq.Vector(0, 0, DOME_Z0), cq.Vector(DOME_R, 0, DOME_Z0))
    dface = cq.Face.makeFromWires(cq.Wire.assembleEdges([dspl, d1, d2]))
    dsolid = cq.Solid.revolve(dface, 360, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1))
    dome = cq.Workplane("XY").add(dsolid)
    stem = (cq.Workplane("XY").workplane(offset=DOME_Z1 - 1.0)
            .circle(STEM_D / 2).extrude(STEM_TOP - DOME_Z1 + 1.0))
    head = band.union(ring).union(dome).union(stem)
    # seams toward the back-left where they are least visible, then place on kingpin
    head = head.rotate((0, 0, 0), (0, 0, 1), 135).translate((STEM_X, 0, 0))
    return head


# ---------------- fork ----------------
def make_fork_plan(z0, h):
    """plan outline of the fork (straight legs, concave blend arcs, rear wrap
    arc around the kingpin) extruded from z0 by h"""
    W, R, xs, rho = LEG_W, SHROUD_R, STEM_X, PLAN_BLEND_R
    V = cq.Vector
    dx = math.sqrt((R + rho) ** 2 - (W + rho) ** 2)
    ux, uy = dx / (R + rho), (W + rho) / (R + rho)

    def side(sg):
        bc = (xs + dx, sg * (W + rho))            # blend arc centre
        t_line = (xs + dx, sg * W)                # blend / leg tangent point
        t_circ = (xs + R * ux, sg * R * uy)       # blend / wrap tangent point
        a1 = math.atan2(t_line[1] - bc[1], t_line[0] - bc[0])
        a2 = math.atan2(t_circ[1] - bc[1], t_circ[0] - bc[0])
        am = 0.5 * (a1 + a2)
        bm = (bc[0] + rho * math.cos(am), bc[1] + rho * math.sin(am))
        return t_line, bm, t_circ

    tl0, bm0, tc0 = side(-1)
    tl1, bm1, tc1 = side(1)

    def P(p):
        return V(p[0], p[1], z0)

    edges = [
        cq.Edge.makeLine(P((FORK_FRONT, -W)), P(tl0)),
        cq.Edge.makeThreePointArc(P(tl0), P(bm0), P(tc0)),
        cq.Edge.makeThreePointArc(P(tc0), P((xs - R, 0.0)), P(tc1)),
        cq.Edge.makeThreePointArc(P(tc1), P(bm1), P(tl1)),
        cq.Edge.makeLine(P(tl1), P((FORK_FRONT, W))),
        cq.Edge.makeLine(P((FORK_FRONT, W)), P((FORK_FRONT, -W))),
    ]
    face = cq.Face.makeFromWires(cq.Wire.assembleEdges(edges))
    return cq.Workplane("XY").add(cq.Solid.extrudeLinear(face, V(0, 0, h)))


def make_fork():
    zb = -30.0
    plan = make_fork_plan(zb, FORK_TOP - zb)
    # round the bend between top plate and the wrap / legs
    plan = plan.edges(cq.selectors.BoxSelector(
        (-200, -200, FORK_TOP - 0.1), (FORK_FRONT - 0.1, 200, FORK_TOP + 0.1))
    ).fillet(BEND_R)
    shell = plan.faces("<Z or >X").shell(-SHEET_T)

    # side profile of the legs (XZ): vertical front edge, rounded end around
    # the axle, straight rear diagonal tangent to the rounded end
    xb = STEM_X - SHROUD_R
    P = (xb, REAR_CUT_Z)
    dP = math.hypot(*P)
    angP = math.atan2(P[1], P[0])
    angT = angP + math.acos(LEG_END_R / dP)
    T = (LEG_END_R * math.cos(angT), LEG_END_R * math.sin(angT))
    ztop = FORK_TOP + 5.0
    slope = (P[1] - T[1]) / (P[0] - T[0])
    x_at_top = T[0] + (ztop - T[1]) / slope
    angT_n = angT % (2 * math.pi)
    ang_mid = (angT_n + 2 * math.pi) / 2.0
    mid = (LEG_END_R * math.cos(ang_mid), LEG_END_R * math.sin(ang_mid))
    side = (
        cq.Workplane("XZ")
        .moveTo(FORK_FRONT + 2, 0)
        .lineTo(FORK_FRONT + 2, ztop)
        .lineTo(x_at_top, ztop)
        .lineTo(T[0], T[1])
        .threePointArc(mid, (LEG_END_R, 0))
        .close()
        .extrude(LEG_W + 10, both=True)
    )
    fork = shell.intersect(side)
    holes = (cq.Workplane("XZ").center(HOLE_X, HOLE_Z).circle(HOLE_D / 2)
             .extrude(LEG_W + 5, both=True))
    fork = fork.cut(holes)
    return fork


# ---------------- axle hardware ----------------
def ycyl(r, y0, y1):
    """cylinder along +Y between y0 and y1 (y1 > y0)"""
    return (cq.Workplane("XZ").circle(r).extrude(-(y1 - y0))
            .translate((0, y0, 0)))


def yhex(af, y0, y1):
    """hex prism along +Y, flats top and bottom"""
    ac = af / math.cos(math.radians(30))
    return (cq.Workplane("XZ").polygon(6, ac).extrude(-(y1 - y0))
            .translate((0, y0, 0)))


def make_hardware():
    leg_in = LEG_W - SHEET_T
    y_wash = HUB_W + HUB_WASHER_T
    y_sp = leg_in - 1.2
    grp = ycyl(HUB_WASHER_R, HUB_W - 0.2, y_wash)
    grp = grp.union(yhex(NUT_AF, y_wash - 0.1, y_sp))
    grp = grp.union(ycyl(WASHER_D / 2, y_sp - 0.1, leg_in + 0.05))
    nut = yhex(NUT_AF, LEG_W - 0.05, LEG_W + NUT_T)
    nut = nut.faces(">Y").edges().chamfer(0.6)
    nut = nut.cut(ycyl(1.3, LEG_W + NUT_T - 1.5, LEG_W + NUT_T + 0.5))
    grp = grp.union(nut)
    parts = grp.union(grp.mirror("XZ"))
    axle = ycyl(AXLE_D / 2, -LEG_W - 0.5, LEG_W + 0.5)
    return parts.union(axle)


wheel = make_wheel()
head = make_head()
fork = make_fork()
hw = make_hardware()

result = fork.union(head).union(hw).union(wheel)

VIEW = {"azimuth": 45, "elevation": 26}
